import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_OUT = 50.0          # outer radius of the cup wall
WALL = 2.0            # side wall thickness
FRONT_T = 1.2         # thickness of the closed front disc
DEPTH = 39.5          # overall depth (front face to open end)
RIM_R = 51.0          # outer radius of the rim at the open end
RIM_W = 5.6           # axial width of the rim
RIM_FILLET = 1.8      # rounding of the rim's outer back edge
RIM_CHAMFER = 1.0     # 45 deg chamfer on the rim's front edge
LIP_CHAMFER = 0.5     # small lead-in chamfer on the inner edge of the mouth

# hexagonal vent pattern: zig-zag of hexes in two staggered rows
# running around the lower half of the wall
HEX_W = 11.1          # vertex-to-vertex size (vertices along the axis)
HEX_H = 9.95          # flat-to-flat size (around the circumference)
HEX_Y_FRONT = 9.8     # axial position (from front face) of front row
HEX_Y_BACK = 20.2     # axial position of back row
HEX_START = 3.6       # angle (deg, from +X toward +Z) of first (back) hex
HEX_HALF_PITCH = 6.8  # angular step between successive zig-zag hexes
HEX_COUNT = 28

# keyhole in the front disc
KEY_Z = -37.2         # centre of round part
KEY_R = 3.35
KEY_SLOT_W = 3.7
KEY_BOTTOM = -46.2    # lowest point of the slot

# snap window in the top of the wall (trapezoid seen from above)
SLOT_Y = 8.9          # from front face
SLOT_LEN_BACK = 9.3
SLOT_LEN_FRONT = 7.1
SLOT_W = 4.0

# internal board clips on the inside of the front disc
CLIP_H = 6.0          # height of clips above the inner face
CLIP_T = 2.0          # clip wall thickness
CORNER_X = 18.0       # corner clips on the +x side
CORNER_X_NEG = -15.0  # corner clips on the -x side
CORNER_Z_TOP = -8.0
CORNER_Z_BOT = -30.0
CLIP_A = 7.0          # leg length of corner clips
UCLIP_X = 8.0         # C-clip on the +x side
UCLIP_X_NEG = -9.0    # C-clip on the -x side
UCLIP_Z = 7.6
UCLIP_T = 2.0         # plate thickness (x)
UCLIP_HT = 7.5        # extent along z
UCLIP_H = 9.5         # height above the disc
UCLIP_LEG = 1.5       # leg width of the bridge
UCLIP_TOP = 1.5       # thickness of the bridge top
UCLIP_BASE = 1.5      # thickness of the frame foot on the disc

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- body ----------------
# revolve a half profile (drawn on -X so the seam sits on the far side)
R_IN = R_OUT - WALL
f = RIM_FILLET
c45 = math.cos(math.radians(45))
prof = (
    cq.Workplane("XY")
    .moveTo(0.0, 0.0)
    .lineTo(-R_OUT, 0.0)
    .lineTo(-R_OUT, DEPTH - RIM_W)
    .lineTo(-RIM_R, DEPTH - RIM_W + RIM_CHAMFER)
    .lineTo(-RIM_R, DEPTH - f)
    .threePointArc((-(RIM_R - f + f * c45), DEPTH - f + f * c45), (-(RIM_R - f), DEPTH))
    .lineTo(-(R_IN + LIP_CHAMFER), DEPTH)
    .lineTo(-R_IN, DEPTH - LIP_CHAMFER)
    .lineTo(-R_IN, FRONT_T)
    .lineTo(0.0, FRONT_T)
    .close()
)
body = prof.revolve(360.0, (0, 0, 0), (0, 1, 0))
SEAM_ROT = -50.0      # move the revolve seam to a near-silhouette spot
body = body.rotate((0, 0, 0), (0, 1, 0), SEAM_ROT)

# ---------------- hex vents ----------------
hex_pts = [
    (HEX_W / 2, 0.0),
    (HEX_W / 4, HEX_H / 2),
    (-HEX_W / 4, HEX_H / 2),
    (-HEX_W / 2, 0.0),
    (-HEX_W / 4, -HEX_H / 2),
    (HEX_W / 4, -HEX_H / 2),
]
cutters = None
for i in range(HEX_COUNT):
    ang = HEX_START - i * HEX_HALF_PITCH
    yc = HEX_Y_BACK if i % 2 == 0 else HEX_Y_FRONT
    h = (
        cq.Workplane("YZ", origin=(R_OUT - WALL - 3.0, 0, 0))
        .polyline(hex_pts)
        .close()
        .extrude(WALL + 6.0)
        .rotate((0, 0, 0), (0, 1, 0), -ang)
        .translate((0, yc, 0))
    )
    cutters = h if cutters is None else cutters.union(h)
body = body.cut(cutters)

# ---------------- keyhole ----------------
key = (
    cq.Workplane("XZ", origin=(0, FRONT_T + 1.0, 0))
    .center(0, KEY_Z)
    .circle(KEY_R)
    .extrude(FRONT_T + 2.0)
)
key_len = KEY_Z - KEY_BOTTOM
key_slot = (
    cq.Workplane("XZ", origin=(0, FRONT_T + 1.0, 0))
    .center(0, (KEY_Z + KEY_BOTTOM) / 2)
    .slot2D(key_len, KEY_SLOT_W, 90)
    .extrude(FRONT_T + 2.0)
)
body = body.cut(key).cut(key_slot)

# ---------------- top snap window ----------------
win = (
    cq.Workplane("XY", origin=(0, 0, R_OUT - WALL - 2.0))
    .polyline([
        (-SLOT_LEN_FRONT / 2, SLOT_Y - SLOT_W / 2),
        (SLOT_LEN_FRONT / 2, SLOT_Y - SLOT_W / 2),
        (SLOT_LEN_BACK / 2, SLOT_Y + SLOT_W / 2),
        (-SLOT_LEN_BACK / 2, SLOT_Y + SLOT_W / 2),
    ])
    .close()
    .extrude(WALL + 5.0)
)
body = body.cut(win)


# ---------------- internal clips ----------------
def box(cx, cz, sx, sz, h=CLIP_H):
    return cq.Workplane("XY").box(sx, h, sz).translate((cx, FRONT_T + h / 2, cz))


def corner_clip(x, z, sx, sz):
    """L / Gamma shaped corner clip; sx, sz = +/-1 give the side of the
    outer leg (x) and of the cross bar (z)."""
    a, t = CLIP_A, CLIP_T
    leg = box(x + sx * (a / 2 - t / 2), z, t, a)
    bar = box(x, z + sz * (a / 2 - t * 0.75), a, t * 1.5)
    return leg.union(bar)


def c_clip(x, z, sx):
    """Cable-tie style clip: an upright plate in the YZ plane with a
    rectangular window through it."""
    t, hz, hy = UCLIP_T, UCLIP_HT, UCLIP_H
    plate = box(x, z, t, hz, hy)
    win_h = hy - UCLIP_TOP - UCLIP_BASE
    win = box(x, z, t + 1.0, hz - 2 * UCLIP_LEG, win_h).translate((0, UCLIP_BASE, 0))
    return plate.cut(win)


clips = None
for sx, cx, ux in ((1, CORNER_X, UCLIP_X), (-1, CORNER_X_NEG, UCLIP_X_NEG)):
    parts = [
        corner_clip(cx, CORNER_Z_TOP, sx, 1),
        corner_clip(cx, CORNER_Z_BOT, sx, -1),
        c_clip(ux, UCLIP_Z, sx),
    ]
    for p in parts:
        clips = p if clips is None else clips.union(p)
body = body.union(clips)

result = body
